import math
import cadquery as cq
from cadquery.occ_impl.shapes import BRepOffsetAPI_ThruSections

# =====================================================================
#  Camera / sensor housing: crowned, tapered oval body with a flat face
#  (+X) carrying a groove-outlined stadium panel (lens bore, crescent
#  indicator slot, 3x3 microphone holes); back face (-X) carries a
#  locating pin and an eyelet lug.
# =====================================================================

# ---------------- body (mm) ----------------
DEPTH = 24.0          # back face x=0 -> front face x=DEPTH
HALF_L_BACK = 40.3    # half length (Y) of the back face
HALF_L_FRONT = 51.0   # half length (Y) of the (unfilleted) front face
TOP_BACK = 15.2       # top of back face (Z)
TOP_FRONT = 22.3      # top at the face (Z)  (crowned profile)
BOT_BACK = -14.9      # bottom of back face (Z)
BOT_FRONT = -23.0     # bottom at the face (Z) (straight chin)
CROWN_P = 2.5         # exponent of the crowned top profile
N_SECTIONS = 7        # loft sections along the depth (analytic section law)
LOFT_MAX_DEG = 2      # piecewise-quadratic loft along the depth
SUPER_N = 3.0         # superellipse exponent of the outline
FRONT_FILLET = 2.0
BACK_FILLET = 0.8

FEAT_Z = 0.1          # vertical centre of the face features

# face panel: stadium outline formed by a narrow groove (panel flush with the face)
PANEL_Y0 = -39.2
PANEL_Y1 = 8.2
PANEL_H = 22.6
GROOVE_W = 0.35
GROOVE_D = 0.5

# lens bore (revolved profile: flat floor, 45 deg chamfer, tapered wall, rounded rim)
LENS_Y = -23.3
LENS_R_TOP = 8.0      # wall radius at the face (virtual sharp rim)
LENS_R_MID = 6.3      # top of the floor chamfer
LENS_R_FLOOR = 5.4    # flat floor radius
LENS_DEPTH = 5.9      # floor depth below the face
LENS_RIM_R = 0.5      # rim round
LENS_PIN_R = 1.2
LENS_PIN_DEPTH = 1.5

# crescent slot
CRES_CY = -30.45      # arc centre (Y)
CRES_R = 6.6          # centreline radius
CRES_HALF_ANG = 35.0  # half angle of arc
CRES_W = 1.56
CRES_DEPTH = 0.8

# microphone grid
MIC_Y = -1.5
MIC_PITCH_Y = 2.19
MIC_PITCH_Z = 2.12
MIC_D = 1.2
MIC_DEPTH = 2.0

# back pin
PIN_Y = 30.7
PIN_Z = 6.7
PIN_D = 3.4
PIN_L = 14.0

# back eyelet lug
LUG_Y = -9.6
LUG_T = 10.4          # thickness along Y
LUG_CX = -3.6         # hole centre behind back face
LUG_R = 4.5
LUG_HOLE_R = 2.9
LUG_BASE_HALF = 5.0


# ---------------- helpers ----------------
def oval_pts(a, b, dz=0.0, n=SUPER_N, count=16):
    """Superellipse outline sampled at 16 points (interpolated by a spline)."""
    pts = []
    e = 2.0 / n
    for i in range(count):
        t = 2.0 * math.pi * i / count
        c, s = math.cos(t), math.sin(t)
        y = a * math.copysign(abs(c) ** e, c)
        z = b * math.copysign(abs(s) ** e, s) + dz
        pts.append((y, z))
    return pts


def oval_wire(x, a, b, dz=0.0):
    vs = [cq.Vector(x, y, z) for (y, z) in oval_pts(a, b, dz)]
    # uniform parametrisation keeps the closed spline symmetric about its seam
    edge = cq.Edge.makeSpline(vs, periodic=True, parameters=list(range(len(vs) + 1)))
    return cq.Wire.assembleEdges([edge])


def section(x):
    """Cross-section of the body at depth x.
    Y half-length and chin vary linearly, the top follows a crowned curve."""
    f = x / DEPTH
    a = HALF_L_BACK + (HALF_L_FRONT - HALF_L_BACK) * f
    top = TOP_BACK + (TOP_FRONT - TOP_BACK) * (1.0 - (1.0 - f) ** CROWN_P)
    bot = BOT_BACK + (BOT_FRONT - BOT_BACK) * f
    return oval_wire(x, a, 0.5 * (top - bot), 0.5 * (top + bot))


# ---------------- main body ----------------
def smooth_loft(wires, max_deg):
    builder = BRepOffsetAPI_ThruSections(True, False)
    builder.SetMaxDegree(max_deg)
    for w in wires:
        builder.AddWire(w.wrapped)
    builder.Build()
    return cq.Solid(builder.Shape())


sections = [section(DEPTH * i / (N_SECTIONS - 1)) for i in range(N_SECTIONS)]
body = cq.Workplane("XY").add(smooth_loft(sections, LOFT_MAX_DEG))
body = body.faces(">X").edges().fillet(FRONT_FILLET)
body = body.faces("<X").edges().fillet(BACK_FILLET)

# ---------------- face panel outline groove ----------------
face_x = DEPTH
panel_len = PANEL_Y1 - PANEL_Y0
panel_cy = 0.5 * (PANEL_Y0 + PANEL_Y1)
groove_outer = (
    cq.Workplane("YZ", origin=(face_x - GROOVE_D, 0, 0))
    .center(panel_cy, FEAT_Z)
    .slot2D(panel_len, PANEL_H)
    .extrude(GROOVE_D + 1.0)
)
groove_inner = (
    cq.Workplane("YZ", origin=(face_x - GROOVE_D - 0.5, 0, 0))
    .center(panel_cy, FEAT_Z)
    .slot2D(panel_len - 2 * GROOVE_W, PANEL_H - 2 * GROOVE_W)
    .extrude(GROOVE_D + 2.0)
)
body = body.cut(groove_outer.cut(groove_inner))


# ---------------- lens bore: revolved profile ----------------
def lens_cutter():
    x_floor = face_x - LENS_DEPTH
    ch = LENS_R_MID - LENS_R_FLOOR                 # 45 deg chamfer size
    # rim round between the tapered wall and the face plane, in (x, r) coordinates
    wall_dir = (-(LENS_DEPTH - ch), -(LENS_R_TOP - LENS_R_MID))  # from rim corner down the wall
    n = math.hypot(*wall_dir)
    d1 = (wall_dir[0] / n, wall_dir[1] / n)
    d2 = (0.0, 1.0)                                 # from rim corner outward along the face
    cos_t = d1[0] * d2[0] + d1[1] * d2[1]
    theta = math.acos(cos_t)
    tdist = LENS_RIM_R / math.tan(theta / 2.0)
    corner = (face_x, LENS_R_TOP)
    t1 = (corner[0] + d1[0] * tdist, corner[1] + d1[1] * tdist)
    t2 = (corner[0] + d2[0] * tdist, corner[1] + d2[1] * tdist)
    bis = (d1[0] + d2[0], d1[1] + d2[1])
    bn = math.hypot(*bis)
    bis = (bis[0] / bn, bis[1] / bn)
    cdist = LENS_RIM_R / math.sin(theta / 2.0)
    centre = (corner[0] + bis[0] * cdist, corner[1] + bis[1] * cdist)
    mid = (centre[0] - bis[0] * LENS_RIM_R, centre[1] - bis[1] * LENS_RIM_R)
    # profile drawn towards -Y so the revolve seam sits on the hidden side of the bore
    plane = cq.Plane(origin=(0, LENS_Y, FEAT_Z), xDir=(1, 0, 0), normal=(0, 0, -1))
    prof = (
        cq.Workplane(plane)
        .moveTo(x_floor, 0.0)
        .lineTo(x_floor, LENS_R_FLOOR)
        .lineTo(x_floor + ch, LENS_R_MID)
        .lineTo(*t1)
        .threePointArc(mid, t2)
        .lineTo(face_x + 1.0, t2[1])
        .lineTo(face_x + 1.0, 0.0)
        .close()
        .revolve(360.0, (0, 0, 0), (1, 0, 0))
    )
    return prof


body = body.cut(lens_cutter())

lens_pin = (
    cq.Workplane("YZ", origin=(face_x - LENS_DEPTH - LENS_PIN_DEPTH, 0, 0))
    .center(LENS_Y, FEAT_Z)
    .circle(LENS_PIN_R)
    .extrude(LENS_PIN_DEPTH + 0.2)
)
body = body.cut(lens_pin)

# ---------------- crescent indicator slot (arc slot) ----------------
a0 = math.radians(180.0 - CRES_HALF_ANG)
a1 = math.radians(180.0)
a2 = math.radians(180.0 + CRES_HALF_ANG)
ro = CRES_R + CRES_W / 2.0
ri = CRES_R - CRES_W / 2.0
hw = CRES_W / 2.0


def P(r, a):
    return (CRES_CY + r * math.cos(a), FEAT_Z + r * math.sin(a))


c0 = P(CRES_R, a0)
c2 = P(CRES_R, a2)
cres = (
    cq.Workplane("YZ", origin=(face_x - CRES_DEPTH, 0, 0))
    .moveTo(*P(ro, a0))
    .threePointArc(P(ro, a1), P(ro, a2))
    .threePointArc(
        (c2[0] + hw * math.cos(a2 + math.pi / 2), c2[1] + hw * math.sin(a2 + math.pi / 2)),
        P(ri, a2),
    )
    .threePointArc(P(ri, a1), P(ri, a0))
    .threePointArc(
        (c0[0] + hw * math.cos(a0 - math.pi / 2), c0[1] + hw * math.sin(a0 - math.pi / 2)),
        P(ro, a0),
    )
    .close()
    .extrude(CRES_DEPTH + 1.0)
)
body = body.cut(cres)

# ---------------- microphone holes 3x3 ----------------
mic_pts = [
    (MIC_Y + i * MIC_PITCH_Y, FEAT_Z + j * MIC_PITCH_Z) for i in (-1, 0, 1) for j in (-1, 0, 1)
]
mics = (
    cq.Workplane("YZ", origin=(face_x - MIC_DEPTH, 0, 0))
    .pushPoints(mic_pts)
    .circle(MIC_D / 2.0)
    .extrude(MIC_DEPTH + 1.0)
)
body = body.cut(mics)

# ---------------- back: locating pin ----------------
pin = (
    cq.Workplane("YZ", origin=(0.5, 0, 0))
    .center(PIN_Y, PIN_Z)
    .circle(PIN_D / 2.0)
    .extrude(-(PIN_L + 0.5))
    .faces("<X").edges().chamfer(0.3)
)
body = body.union(pin)

# ---------------- back: eyelet lug (D profile in XZ, hole along Y) ----------------
lug = (
    cq.Workplane("XZ", origin=(0, LUG_Y + LUG_T / 2.0, 0))
    .moveTo(0.8, LUG_BASE_HALF)
    .lineTo(0.0, LUG_BASE_HALF)
    .lineTo(LUG_CX, LUG_R)
    .threePointArc((LUG_CX - LUG_R, 0.0), (LUG_CX, -LUG_R))
    .lineTo(0.0, -LUG_BASE_HALF)
    .lineTo(0.8, -LUG_BASE_HALF)
    .close()
    .extrude(LUG_T)
)
hole = (
    cq.Workplane("XZ", origin=(0, LUG_Y + LUG_T / 2.0 + 1, 0))
    .center(LUG_CX, 0)
    .circle(LUG_HOLE_R)
    .extrude(LUG_T + 2)
)
lug = lug.cut(hole)
body = body.union(lug)

result = body
